import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_OUT = 14.7          # outer radius of the shank (cylinder, axis along Y)
R_HOLE = 9.0          # finger hole radius
HOLE_DZ = -2.85       # hole centre offset (Z) from the outer-cylinder centre
HW_BOTTOM = 4.95      # half width of the band at the very bottom (Y)
HW_TOP = 9.75         # half width of the band where it meets the bezel (Y)
DISC_D = 30.7         # signet bezel diameter
DISC_T = 2.8          # bezel thickness
DISC_Z0 = 8.95        # underside of the bezel (Z)
FIL_HOLE = 0.85       # fillet on the finger-hole edges
FIL_SIDE = 0.8        # fillet on the outer band edges
FIL_DISC = 0.2        # small fillet on the bezel top and bottom edges
ENGRAVE_D = 0.45      # depth of the bee engraving

DISC_Z1 = DISC_Z0 + DISC_T

# ---------------- shank ----------------
# tapered band: trapezoid in the YZ plane, extruded along X, intersected with
# the outer cylinder
z_bot = -R_OUT - 1.0
z_top = DISC_Z0 + 1.0
slope = (HW_TOP - HW_BOTTOM) / (DISC_Z0 + R_OUT)


def hw(z):
    return HW_BOTTOM + (z + R_OUT) * slope


wedge = (
    cq.Workplane("YZ")
    .polyline([(-hw(z_bot), z_bot), (hw(z_bot), z_bot),
               (hw(z_top), z_top), (-hw(z_top), z_top)])
    .close()
    .extrude(2 * R_OUT + 4, both=True)
)

outer = (
    cq.Workplane("XZ")
    .circle(R_OUT)
    .extrude(2 * HW_TOP + 6, both=True)
)

band = outer.intersect(wedge)

# outer band edges (cylinder / side plane intersections)
band = band.edges(cq.selectors.BoxSelector((-R_OUT - 1, -HW_TOP - 3, -R_OUT - 1),
                                           (R_OUT + 1, HW_TOP + 3, DISC_Z0 - 0.5))).fillet(FIL_SIDE)

hole = (
    cq.Workplane("XZ", origin=(0, 0, HOLE_DZ))
    .circle(R_HOLE)
    .extrude(2 * HW_TOP + 6, both=True)
)
band = band.cut(hole)

# fillet the hole rims: edges lying on the hole cylinder
hole_edges = []
for e in band.edges().vals():
    c = e.Center()
    bb = e.BoundingBox()
    if (abs(bb.xlen - 2 * R_HOLE) < 0.3 and bb.zmax < HOLE_DZ + R_HOLE + 0.3
            and abs(c.y) > 1.0 and e.geomType() != "LINE"):
        hole_edges.append(e)
band = band.newObject(hole_edges).fillet(FIL_HOLE)

# ---------------- bezel ----------------
disc = (
    cq.Workplane("XY", origin=(0, 0, DISC_Z0))
    .circle(DISC_D / 2)
    .extrude(DISC_T)
    .edges().fillet(FIL_DISC)
    .rotate((0, 0, 0), (0, 0, 1), 180)   # keep the circular seam at the back
)

ring = band.union(disc)

# ---------------- bee engraving ----------------
# the bee is engraved as shallow pockets in the bezel top (stinger towards +Y)

# strokes: polylines drawn with a round-ended pen of the given width
STROKES = [
    # left wing: curved upper arm, three vein strips, lower stroke
    ([(-5.6, 3.4), (-3.85, 2.65), (-2.65, 1.75), (-2.4, 0.7), (-1.5, -0.85)], 0.45),
    ([(-6.05, 1.6), (-4.41, 0.0)], 0.34),
    ([(-4.73, 0.9), (-3.09, -0.72)], 0.34),
    ([(-3.25, -0.03), (-1.61, -1.64)], 0.34),
    ([(-5.15, -0.8), (-1.95, -2.15)], 0.45),
    # right wing
    ([(5.25, 3.9), (3.75, 3.5), (2.7, 2.45), (2.55, 1.25), (1.65, -0.35)], 0.45),
    ([(6.05, 1.6), (4.41, 0.0)], 0.34),
    ([(4.73, 0.9), (3.09, -0.72)], 0.34),
    ([(3.25, -0.03), (1.61, -1.64)], 0.34),
    ([(5.15, -0.3), (2.2, -1.75)], 0.45),
    # legs
    ([(-4.3, -4.1), (-2.2, -2.65)], 0.45),
    ([(-3.5, -6.55), (-2.55, -5.0), (-1.6, -3.75)], 0.5),
    ([(-2.7, -7.6), (-1.75, -7.7), (-0.95, -6.4), (-0.4, -4.5)], 0.5),
    ([(2.55, -2.35), (3.95, -3.05)], 0.45),
    ([(2.0, -3.6), (3.05, -5.0), (3.95, -6.1)], 0.5),
    ([(0.8, -4.1), (1.6, -5.5), (2.7, -6.9), (3.35, -7.45)], 0.5),
    # stinger
    ([(-0.5, 6.7), (-0.25, 6.35), (0.75, 5.6)], 0.4),
    ([(0.8, 5.55), (1.55, 5.15)], 0.3),
]
# lobes: rotated ellipses (x, y, semi-axis a, semi-axis b, angle deg)
LOBES = [
    (-6.65, 1.62, 1.45, 0.42, -50.0),
    (6.65, 1.62, 1.45, 0.42, 50.0),
    (-0.5, 6.65, 0.38, 0.45, 0.0),
    (0.1, -0.92, 0.95, 0.83, 0.0),
    (-1.4, -2.9, 0.22, 0.38, -20.0),
    (1.7, -2.8, 0.22, 0.38, 20.0),
]
# rounded body segments: (x, y, width, height, corner radius)
SEGMENTS = [
    (0.0, 4.95, 2.5, 0.75, 0.3),
    (0.0, 3.7, 3.2, 0.95, 0.4),
    (0.0, 2.41, 3.3, 0.96, 0.4),
    (0.0, 0.96, 2.7, 1.05, 0.42),
    (0.15, -2.7, 2.05, 1.35, 0.5),
    (0.05, -4.05, 1.6, 0.9, 0.38),
]

sk = cq.Sketch()
for pts, w in STROKES:
    for (x1, y1), (x2, y2) in zip(pts[:-1], pts[1:]):
        L = math.hypot(x2 - x1, y2 - y1)
        ang = math.degrees(math.atan2(y2 - y1, x2 - x1))
        sk = sk.push([((x1 + x2) / 2, (y1 + y2) / 2)]).slot(L, w, angle=ang).reset()
for (x, y, a, b, ang) in LOBES:
    sk = sk.push([(x, y)]).ellipse(a, b, angle=ang).reset()

z_eng = DISC_Z1 - ENGRAVE_D
engr = (
    cq.Workplane("XY", origin=(0, 0, z_eng))
    .placeSketch(sk)
    .extrude(ENGRAVE_D + 1.0)
)
for (x, y, w, h, r) in SEGMENTS:
    seg = (
        cq.Workplane("XY", origin=(x, y, z_eng))
        .rect(w, h)
        .extrude(ENGRAVE_D + 1.0)
        .edges("|Z").fillet(r)
    )
    engr = engr.union(seg)

ring = ring.cut(engr)

result = ring

VIEW = {"azimuth": 45, "elevation": 26}
